import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
N = 4                 # cells per side (4 x 4 grid)
W = 240.0             # cell-grid width / depth (pitch basis)
T = 7.5               # overall thickness of the tray
P = W / N             # cell pitch
RIB_TOP = 2.2         # flat top width of the divider ribs
RIM_TOP = 1.4         # flat top width of the outer rim
H_UP = 2.9            # height of the upper drafted flank of each cell
H_MID = 2.4           # height of the vertical middle band
DRAFT = 31.0          # flank draft from vertical (deg), upper and lower flank
R_TOP = 4.2           # corner radius of the cell openings at the top face
EDGE_BOT = 0.8        # small round on the outer bottom edge

# ---------------- derived ----------------
H_LOW = T - H_UP - H_MID          # height of the lower drafted flank
tn = math.tan(math.radians(DRAFT))
DX_UP = H_UP * tn                 # inward step of the upper flank
DX_LOW = H_LOW * tn               # inward step of the lower flank
A_TOP = (P - RIB_TOP) / 2         # half size of a cell opening at the top face
A_MID = A_TOP - DX_UP             # half size along the vertical band
R_MID = R_TOP - DX_UP             # corner radius along the vertical band
WO = W + 2 * (RIM_TOP - RIB_TOP / 2)   # outside size of the tray
R_OUT = R_TOP + RIM_TOP           # outer corner radius (concentric with cells)
EPS = 0.5                         # cutter overshoot above / below the part


def rounded_face(z, half, r, down):
    """workplane at height z (normal up or down) holding a rounded-square sketch"""
    pl = cq.Plane(origin=(0, 0, z), xDir=(1, 0, 0),
                  normal=(0, 0, -1) if down else (0, 0, 1))
    return cq.Workplane(pl).sketch().rect(2 * half, 2 * half).vertices().fillet(r).finalize()


def cell_cutter():
    """void of one cell, centred on the origin:
    drafted upper flank -> vertical band -> drafted lower flank"""
    up = rounded_face(T + EPS, A_TOP + EPS * tn, R_TOP + EPS * tn, True) \
        .extrude(H_UP + EPS, taper=DRAFT)
    mid = rounded_face(H_LOW, A_MID, R_MID, False).extrude(H_MID + 0.2)
    low = rounded_face(H_LOW, A_MID, R_MID, True).extrude(H_LOW + EPS, taper=DRAFT)
    return up.union(mid).union(low).val()


# outer body: rounded square slab, sharp top edge, softened bottom edge
body = (cq.Workplane("XY")
        .sketch().rect(WO, WO).vertices().fillet(R_OUT).finalize()
        .extrude(T))
body = body.faces("<Z").edges().fillet(EDGE_BOT)

# 4 x 4 rectangular pattern of cell voids
proto = cell_cutter()
cutters = [proto.translate(cq.Vector(-W / 2 + P / 2 + i * P, -W / 2 + P / 2 + j * P, 0))
           for i in range(N) for j in range(N)]
body = body.cut(cq.Workplane("XY").add(cq.Compound.makeCompound(cutters)))

result = body
